import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 83.0          # box width  (X)
L = 131.0         # box length (Y)
H = 42.0          # box height (Z)
R_CORNER = 3.5    # vertical corner radius
T_WALL = 2.5      # side wall thickness
T_FLOOR = 2.5     # floor thickness
T_LID = 3.0       # lid (top plate) thickness
TOP_FILLET = 1.0  # top perimeter edge round
BOT_CHAMFER = 1.0 # bottom perimeter chamfer
SEAM_Z = H - T_LID  # lid / body seam height
SEAM_D = 0.25     # seam groove depth
SEAM_H = 0.25     # seam groove height

# corner lid screws
CORNER_INSET = 6.7
CORNER_HOLE_D = 2.9
BOSS_R = 4.0
CORNER_HOLE_DEPTH = 14.0

# stepped vertical bores in the two back corners of the body (they break out
# through the rounded corner skin just below the lid seam)
BACK_BORE_D1 = 4.0       # upper (counterbore) diameter
BACK_BORE_H1 = 10.5      # upper depth below the seam
BACK_BORE_D2 = 2.4       # lower (pilot) diameter
BACK_BORE_H2 = 7.0       # pilot depth
BACK_BORE_SKIN = 0.76    # bore axis distance inside the outer corner surface
BACK_WEB = 4.6           # solid corner web (measured from the outer faces) around the bore

# top panel features (X, Y on the lid)
RECT_Y = -44.5
RECT_OUT = (27.3, 16.1)   # window outline on the lid top
RECT_TAPER = 2.2          # depth of the tapered (drafted) part of the window
RECT_INSET = 2.08         # horizontal inset of the drafted walls over that depth
RECT_IN = (RECT_OUT[0] - 2 * RECT_INSET, RECT_OUT[1] - 2 * RECT_INSET)  # straight through part
BIG_TOP_D = 16.0
BIG_TOP_Y = -19.1
SMALL_TOP_D = 5.8
SMALL_TOP_Y = 2.35
BACK_TOP_D = 8.8
BACK_TOP_Y = 41.3

RIB_W = 1.0
RIB_H = 0.5
# half of the symmetric rib logo (left side, X<0); mirrored for right side
RIBS_LEFT = [
    [(-13.3, 29.55), (-10.45, 29.55), (-8.45, 32.05)],  # "arm"
    [(-3.05, 28.95), (-6.07, 18.05), (-10.65, 18.05)],  # "leg"
]

# side panel connector holes (same on +X and -X faces)
SIDE_Z = 19.5
SIDE_HOLES = [(-15.0, 23.5, True), (19.2, 21.4, True), (48.05, 10.8, False)]  # (Y, dia, has screws)
SCREW_D = 3.2
SCREW_DY = 9.2
SCREW_DZ = 11.6

# ---------------- outer shell ----------------
outer = (
    cq.Workplane("XY")
    .box(W, L, H, centered=(True, True, False))
    .edges("|Z").fillet(R_CORNER)
    .faces(">Z").edges().fillet(TOP_FILLET)
    .faces("<Z").edges().chamfer(BOT_CHAMFER)
)

# interior cavity
cav_h = H - T_LID - T_FLOOR
cavity = (
    cq.Workplane("XY")
    .workplane(offset=T_FLOOR)
    .rect(W - 2 * T_WALL, L - 2 * T_WALL)
    .extrude(cav_h)
    .edges("|Z").fillet(max(R_CORNER - T_WALL, 0.5))
)
body = outer.cut(cavity)

# corner screw bosses inside the cavity
cx = W / 2 - CORNER_INSET
cy = L / 2 - CORNER_INSET
corner_pts = [(sx * cx, sy * cy) for sx in (-1, 1) for sy in (-1, 1)]
bosses = (
    cq.Workplane("XY")
    .workplane(offset=T_FLOOR)
    .pushPoints(corner_pts)
    .circle(BOSS_R)
    .extrude(cav_h)
)
# keep bosses inside the outer envelope
bosses = bosses.intersect(
    cq.Workplane("XY").box(W, L, H, centered=(True, True, False)).edges("|Z").fillet(R_CORNER)
)
body = body.union(bosses)

# lid seam groove all around
seam_outer = (
    cq.Workplane("XY").workplane(offset=SEAM_Z - SEAM_H / 2)
    .rect(W + 2, L + 2).extrude(SEAM_H)
)
seam_inner = (
    cq.Workplane("XY").workplane(offset=SEAM_Z - SEAM_H / 2)
    .rect(W - 2 * SEAM_D, L - 2 * SEAM_D).extrude(SEAM_H)
    .edges("|Z").fillet(R_CORNER - SEAM_D)
)
body = body.cut(seam_outer.cut(seam_inner))

# back corner bores
for sx in (-1, 1):
    acx = sx * (W / 2 - R_CORNER)
    acy = L / 2 - R_CORNER
    k = (R_CORNER - BACK_BORE_SKIN) / math.sqrt(2.0)
    bx, by = acx + sx * k, acy + k
    # solid corner web around the bore inside the cavity
    web = (
        cq.Workplane("XY").workplane(offset=SEAM_Z - BACK_BORE_H1 - BACK_BORE_H2 - 1.0)
        .center(sx * (W / 2 - BACK_WEB / 2), L / 2 - BACK_WEB / 2)
        .rect(BACK_WEB, BACK_WEB)
        .extrude(BACK_BORE_H1 + BACK_BORE_H2 + 1.0 + T_LID - 0.5)
    )
    body = body.union(web.intersect(cavity))
    bore1 = (
        cq.Workplane("XY").workplane(offset=SEAM_Z)
        .center(bx, by).circle(BACK_BORE_D1 / 2).extrude(-BACK_BORE_H1)
    )
    bore2 = (
        cq.Workplane("XY").workplane(offset=SEAM_Z - BACK_BORE_H1 + 0.01)
        .center(bx, by).circle(BACK_BORE_D2 / 2).extrude(-BACK_BORE_H2)
    )
    body = body.cut(bore1).cut(bore2)

# ---------------- top panel features ----------------
top = cq.Workplane("XY").workplane(offset=H)

# corner screw holes through the lid into the bosses
body = body.cut(
    top.pushPoints(corner_pts).circle(CORNER_HOLE_D / 2).extrude(-CORNER_HOLE_DEPTH)
)

# tapered rectangular window: drafted walls from the top outline down to the
# smaller opening, which then continues straight through the lid
taper_ang = math.degrees(math.atan2(RECT_INSET, RECT_TAPER))
taper = (
    cq.Workplane("XY").workplane(offset=-H, invert=True)   # plane on the lid top, normal -Z
    .center(0, -RECT_Y)                                     # (Y axis is flipped on this plane)
    .rect(*RECT_OUT)
    .extrude(RECT_TAPER, taper=taper_ang)
)
body = body.cut(taper)
body = body.cut(top.center(0, RECT_Y).rect(*RECT_IN).extrude(-T_LID - 1))

# round holes on the lid
for d, y in ((BIG_TOP_D, BIG_TOP_Y), (SMALL_TOP_D, SMALL_TOP_Y), (BACK_TOP_D, BACK_TOP_Y)):
    body = body.cut(top.center(0, y).circle(d / 2).extrude(-T_LID - 1))

# raised rib logo: each rib is a mitred outline around a centre polyline
def rib_outline(pts, w):
    hw = w / 2.0
    segs = []
    for (ax, ay), (bx, by) in zip(pts[:-1], pts[1:]):
        dx, dy = bx - ax, by - ay
        ln = math.hypot(dx, dy)
        segs.append((dx / ln, dy / ln))
    normals = [(-dy, dx) for (dx, dy) in segs]
    left, right = [], []
    for i, (px, py) in enumerate(pts):
        if i == 0:
            nx, ny = normals[0]
            sc = 1.0
        elif i == len(pts) - 1:
            nx, ny = normals[-1]
            sc = 1.0
        else:
            ax, ay = normals[i - 1]
            bx, by = normals[i]
            mx, my = ax + bx, ay + by
            ml = math.hypot(mx, my)
            nx, ny = mx / ml, my / ml
            sc = 1.0 / (nx * ax + ny * ay)
        left.append((px + nx * hw * sc, py + ny * hw * sc))
        right.append((px - nx * hw * sc, py - ny * hw * sc))
    return left + right[::-1]

ribs = None
for poly in RIBS_LEFT:
    for sgn in (1, -1):
        pts = [(sgn * x, y) for (x, y) in poly]
        outline = rib_outline(pts, RIB_W)
        rib = (
            cq.Workplane("XY").workplane(offset=H - 0.01)
            .polyline(outline).close()
            .extrude(RIB_H + 0.01)
        )
        ribs = rib if ribs is None else ribs.union(rib)
body = body.union(ribs)

# ---------------- side connector holes ----------------
for side in (1, -1):
    for (y, d, screws) in SIDE_HOLES:
        cut = (
            cq.Workplane("YZ").workplane(offset=side * (W / 2 + 1))
            .center(y, SIDE_Z).circle(d / 2)
            .extrude(-side * (T_WALL + 3))
        )
        body = body.cut(cut)
        if screws:
            # diagonal pattern, upper-left / lower-right as seen from outside
            pts = [(y - side * SCREW_DY, SIDE_Z + SCREW_DZ), (y + side * SCREW_DY, SIDE_Z - SCREW_DZ)]
            sc = (
                cq.Workplane("YZ").workplane(offset=side * (W / 2 + 1))
                .pushPoints(pts).circle(SCREW_D / 2)
                .extrude(-side * (T_WALL + 3))
            )
            body = body.cut(sc)

result = body
